import math

import cadquery as cq
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge, BRepBuilderAPI_MakeWire
from OCP.GC import GC_MakeArcOfCircle, GC_MakeSegment
from OCP.GeomConvert import GeomConvert_CompCurveToBSplineCurve
from OCP.gp import gp_Pnt

# Square-hole gauge plate: a thin rectangular plate (chamfered corners) with
# 29 square through-holes with rounded corners.  The hole sizes step from
# HOLE_MIN upward in HOLE_STEP increments (7 mm .. 35 mm).
#   row 1 (back edge) : 7 .. 17 mm, small to large, left to right
#   row 2             : 18 .. 24 mm, large on the left
#   row 3             : 25 .. 30 mm, left to right
#   row 4 (front edge): 31 .. 35 mm, left to right

# ---------------- driving dimensions (mm) ----------------
PLATE_L = 200.0        # along X
PLATE_W = 120.0        # along Y
PLATE_T = 2.5          # thickness (Z)
PLATE_CORNER_C = 2.0   # 45 deg chamfer on the four vertical plate corners

HOLE_MIN = 7.0         # smallest square hole
HOLE_STEP = 1.0        # size increment from one hole to the next
HOLE_R = 3.0           # corner radius of the square holes

# hole layout: (centre x, centre y, index in the size sequence)
HOLE_LAYOUT = [
    # row 1 (back edge)
    (-76.2, 52.8, 0), (-66.2, 52.1, 1), (-55.5, 52.5, 2), (-41.4, 51.2, 3),
    (-28.0, 51.0, 4), (-13.9, 50.2, 5), (2.6, 49.65, 6), (18.85, 49.2, 7),
    (35.7, 49.6, 8), (53.25, 48.85, 9), (72.8, 48.8, 10),
    # row 2 (bottom edges aligned, largest on the left)
    (-72.55, 31.9, 17), (-46.6, 31.5, 16), (-21.2, 31.0, 15), (2.8, 30.4, 14),
    (28.3, 30.0, 13), (51.2, 29.6, 12), (72.8, 29.1, 11),
    # row 3
    (-83.2, 3.2, 18), (-53.3, 1.0, 19), (-22.8, 2.65, 20), (7.7, 2.2, 21),
    (39.45, 1.8, 22), (73.0, 1.25, 23),
    # row 4 (front edge)
    (-79.7, -32.3, 24), (-45.3, -32.6, 25), (-6.9, -33.15, 26), (29.7, -33.65, 27),
    (70.6, -35.5, 28),
]
HOLES = [(x, y, HOLE_MIN + i * HOLE_STEP) for (x, y, i) in HOLE_LAYOUT]


def rounded_square_wire(x, y, s, r, z=0.0):
    """Closed rounded-square profile: 4 straight sides + 4 tangent corner arcs,
    joined exactly (no approximation) into one smooth NURBS edge so that each
    hole wall is a single continuous face."""
    h = s / 2.0
    r = min(r, h - 1e-3)
    a = h - r                                   # half length of straight side
    d = r * (1.0 - 1.0 / math.sqrt(2.0))        # arc mid-point inset

    def P(px, py):
        return gp_Pnt(x + px, y + py, z)

    pieces = [
        GC_MakeSegment(P(0, -h), P(a, -h)).Value(),
        GC_MakeArcOfCircle(P(a, -h), P(h - d, -h + d), P(h, -a)).Value(),
        GC_MakeSegment(P(h, -a), P(h, a)).Value(),
        GC_MakeArcOfCircle(P(h, a), P(h - d, h - d), P(a, h)).Value(),
        GC_MakeSegment(P(a, h), P(-a, h)).Value(),
        GC_MakeArcOfCircle(P(-a, h), P(-h + d, h - d), P(-h, a)).Value(),
        GC_MakeSegment(P(-h, a), P(-h, -a)).Value(),
        GC_MakeArcOfCircle(P(-h, -a), P(-h + d, -h + d), P(-a, -h)).Value(),
        GC_MakeSegment(P(-a, -h), P(0, -h)).Value(),
    ]
    joiner = GeomConvert_CompCurveToBSplineCurve()
    for piece in pieces:
        joiner.Add(piece, 1e-7)
    edge = BRepBuilderAPI_MakeEdge(joiner.BSplineCurve()).Edge()
    return cq.Wire(BRepBuilderAPI_MakeWire(edge).Wire())


def hole_cutter(x, y, s):
    """Through-cut prism with the rounded-square cross-section."""
    profile = cq.Face.makeFromWires(rounded_square_wire(x, y, s, HOLE_R, -PLATE_T))
    return cq.Solid.extrudeLinear(profile, cq.Vector(0, 0, 3.0 * PLATE_T))


# ---------------- plate ----------------
plate = (
    cq.Workplane("XY")
    .rect(PLATE_L, PLATE_W)
    .extrude(PLATE_T)
    .edges("|Z")
    .chamfer(PLATE_CORNER_C)
)

# ---------------- square gauge holes (all cut in one boolean) ----------------
cutters = cq.Compound.makeCompound([hole_cutter(x, y, s) for (x, y, s) in HOLES])
result = plate.cut(cutters)

VIEW = {"azimuth": 45, "elevation": 26}
